import math
import cadquery as cq

# ------------------------------------------------------------------
# Forked arm bracket: two parallel side plates (with a clevis fork at
# the upper-left), joined by a solid upper block, a solid lower tip
# block and a central spacer.  Three bolt stations: counterbores on the
# front (-Y) plate, hex-nut pockets on the back (+Y) plate.
# Plates are parallel to the XZ plane; width runs along Y.
# ------------------------------------------------------------------

# ---------------- driving dimensions (mm) ----------------
W = 78.4            # overall width across both plates (Y)
T = 6.2             # plate thickness
GAP = W - 2 * T     # clear gap between plates
CH = 7.0            # 45 deg chamfer where the blocks meet the plates

BIG_D = 7.6         # bolt hole diameter
CB_D = 14.0         # counterbore diameter (front plate)
CB_DEPTH = 10.0
CB_CH = 0.6         # entry chamfer on counterbores
HEX_AF = 13.0       # hex nut pocket across flats (back plate)
HEX_DEPTH = 8.0
HEX_ROT = 40.0      # hex pocket orientation (deg, vertex angle in XZ)
HEX_R = HEX_AF / math.sqrt(3.0)
SMALL_D = 5.5       # fork mounting holes

PIN_R = 13.3        # central spacer radius
PIN_FLARE = 6.5     # conical flare of spacer into each plate

TOP_R = 5.5         # radius of the rounded underside of the upper block
FILLET_R = 4.0      # rounding of the tip corners
BEND_R = 8.0        # rounding of the bend on the +X edge

TIP_Y = 11.5        # half width of the flat tip end after the tip chamfers
TIP_FILLET = 5.0    # rounding of the chisel chamfer edges


# The side profile was laid out on a drawing grid (u right, v down);
# P() maps it to model X (right) / Z (up).
def P(u, v):
    return (u - 400.0, 130.0 - v)


# ---------------- side profile (drawing grid) ----------------
top_v = 11.2          # top edge of upper fork finger
fork_u = 303.4        # fork finger tips
fin_ch = 4.6          # chamfer on finger tips
U_u = 351.7           # bottom of the fork slot
fin1_bot = 28.8
fin2_top = 73.4
fin2_bot = 90.5
bend = (430.0, 55.0)          # corner between upper diagonal and steep edge
steep_k = 0.253               # du/dv along the steep (+X) edge
ll_top = (368.5, 105.4)       # start of the lower-left edge
ll_k = 0.647                  # du/dv along the lower-left edge
tip_a = (477.1, 240.5)        # steep edge meets tip end
tip_b = (462.2, 250.3)        # tip end meets lower-left edge


def steep_u(v):
    return bend[0] + steep_k * (v - bend[1])


def ll_u(v):
    return ll_top[0] + ll_k * (v - ll_top[1])


profile_pts = [
    P(fork_u, top_v + fin_ch),
    P(fork_u + fin_ch, top_v),
    P(366.2, top_v),
    P(*bend),
    P(*tip_a),
    P(*tip_b),
    P(*ll_top),
    P(346.9, fin2_bot),
    P(fork_u + fin_ch, fin2_bot),
    P(fork_u, fin2_bot - fin_ch),
    P(fork_u, fin2_top),
    P(U_u, fin2_top),
    P(U_u, fin1_bot),
    P(fork_u, fin1_bot),
]

# bolt stations
H_top = P(420.9, 62.7)
H_mid = P(399.4, 132.4)
H_bot = P(459.2, 221.2)
PIN_C = P(397.0, 134.6)        # spacer axis

# fork holes
small_holes = [P(u, v) for u in (312.45, 330.2, 348.0) for v in (21.0, 80.9)]
small_holes += [P(359.4, 33.2), P(359.4, 68.8)]

# upper block: rounded underside (circle) starting on the upper diagonal edge
TOP_START_U = 419.5
TOP_START = (TOP_START_U, top_v + (bend[1] - top_v) * (TOP_START_U - 366.2) / (bend[0] - 366.2))
TOP_C = (415.2, 64.9)
# lower block: inclined inner face
BOT_V_STEEP = 200.5
BOT_V_LL = 218.3


# ---------------- helpers ----------------
def xz_wp(y0, flip=False):
    """Workplane parallel to XZ at Y=y0. Normal +Y (or -Y if flip)."""
    n = (0, -1, 0) if flip else (0, 1, 0)
    return cq.Workplane(cq.Plane(origin=(0, y0, 0), xDir=(1, 0, 0), normal=n))


def Lp(p):          # model (X,Z) -> local coords for normal +Y plane (local y = -Z)
    return (p[0], -p[1])


def Ln(p):          # model (X,Z) -> local coords for normal -Y plane (local y = +Z)
    return (p[0], p[1])


def near(q, r=2.0):
    return cq.selectors.BoxSelector((q[0] - r, -W, q[1] - r), (q[0] + r, W, q[1] + r))


# ---------------- outer envelope ----------------
outer = xz_wp(-W / 2).polyline([Lp(p) for p in profile_pts]).close().extrude(W)
outer = outer.edges("|Y").edges(near(P(*bend))).fillet(BEND_R)
for corner in (tip_a, tip_b):
    outer = outer.edges("|Y").edges(near(P(*corner))).fillet(FILLET_R)

# ---------------- cavity between the plates ----------------
# upper block boundary: straight run from TOP_START (on the upper diagonal edge)
# tangent to a circle, around the circle's underside, out through the steep face
tdx, tdz = TOP_C[0] - TOP_START[0], TOP_C[1] - TOP_START[1]
td = math.hypot(tdx, tdz)
t_ang = math.atan2(tdz, tdx) + math.asin(TOP_R / td)     # tangent on the -X side
t_len = math.sqrt(td * td - TOP_R * TOP_R)
tan_pt = (TOP_START[0] + t_len * math.cos(t_ang), TOP_START[1] + t_len * math.sin(t_ang))


def on_top_circle(deg):
    a = math.radians(deg)
    return (TOP_C[0] + TOP_R * math.cos(a), TOP_C[1] + TOP_R * math.sin(a))


a_tan = math.degrees(math.atan2(tan_pt[1] - TOP_C[1], tan_pt[0] - TOP_C[0]))
if a_tan < 0:
    a_tan += 360.0
arc_end = on_top_circle(90.0)                 # lowest point of the rounded underside
arc_mid = on_top_circle((a_tan + 90.0) / 2.0)

# outward normal of upper diagonal edge (drawing grid, pointing up/right)
ue = (bend[0] - 366.2, bend[1] - top_v)
uel = math.hypot(*ue)
un = (ue[1] / uel, -ue[0] / uel)

# lower block boundary: line from steep edge to lower-left edge, extended outside
b_r = (steep_u(BOT_V_STEEP), BOT_V_STEEP)
b_l = (ll_u(BOT_V_LL), BOT_V_LL)
bd = ((b_l[0] - b_r[0]), (b_l[1] - b_r[1]))
bdl = math.hypot(*bd)
bd = (bd[0] / bdl, bd[1] / bdl)
b_out = (b_l[0] + 25 * bd[0], b_l[1] + 25 * bd[1])
b_in = (b_r[0] - 25 * bd[0], b_r[1] - 25 * bd[1])

far = 60.0
cav_pts_grid = {
    "s0": (TOP_START[0] + far * un[0], TOP_START[1] + far * un[1]),
    "s1": TOP_START,
    "tp": tan_pt,
    "am": arc_mid,
    "ae": arc_end,
    "r0": (arc_end[0] + 40, arc_end[1]),
    "r1": (b_in[0] + 15, b_in[1]),
    "bi": b_in,
    "bo": b_out,
    "l0": (b_out[0] - 80, b_out[1] + 40),
    "l1": (200.0, 400.0),
    "l2": (200.0, -100.0),
    "l3": (TOP_START[0] + far * un[0], -100.0),
}
C = {k: P(*v) for k, v in cav_pts_grid.items()}


def cav_sketch(wp, Lf):
    return (
        wp.moveTo(*Lf(C["s0"]))
        .lineTo(*Lf(C["s1"]))
        .lineTo(*Lf(C["tp"]))
        .threePointArc(Lf(C["am"]), Lf(C["ae"]))
        .lineTo(*Lf(C["r0"]))
        .lineTo(*Lf(C["r1"]))
        .lineTo(*Lf(C["bi"]))
        .lineTo(*Lf(C["bo"]))
        .lineTo(*Lf(C["l0"]))
        .lineTo(*Lf(C["l1"]))
        .lineTo(*Lf(C["l2"]))
        .lineTo(*Lf(C["l3"]))
        .close()
    )


# straight middle part + 45 deg drafted ends -> chamfers where blocks meet plates
cav = cav_sketch(xz_wp(-GAP / 2 + CH), Lp).extrude(GAP - 2 * CH)
cav = cav.union(cav_sketch(xz_wp(GAP / 2 - CH), Lp).extrude(CH, taper=45))
cav = cav.union(cav_sketch(xz_wp(-GAP / 2 + CH, flip=True), Ln).extrude(CH, taper=45))

body = outer.cut(cav)

# ---------------- central spacer with conical flares ----------------
pin = (
    cq.Workplane("XY")
    .polyline([(0, -GAP / 2), (PIN_R + PIN_FLARE, -GAP / 2), (PIN_R, -GAP / 2 + PIN_FLARE),
               (PIN_R, GAP / 2 - PIN_FLARE), (PIN_R + PIN_FLARE, GAP / 2), (0, GAP / 2)])
    .close()
    .revolve(360, (0, 0, 0), (0, 1, 0))
    .translate((PIN_C[0], 0, PIN_C[1]))
    .intersect(outer)
)
body = body.union(pin)

# ---------------- chisel chamfers on the tip ----------------
c1 = P(454.2, 234.2)          # chamfer start line on the plate faces
c2 = P(471.9, 226.5)
tip_end = P(465.0, 248.5)
ux, uz = c2[0] - c1[0], c2[1] - c1[1]
ul = math.hypot(ux, uz)
ux, uz = ux / ul, uz / ul
nx, nz = uz, -ux
if (tip_end[0] - c1[0]) * nx + (tip_end[1] - c1[1]) * nz < 0:
    nx, nz = -nx, -nz
ndist = (tip_end[0] - c1[0]) * nx + (tip_end[1] - c1[1]) * nz
for side in (-1, 1):
    y_face = side * W / 2
    y_end = side * TIP_Y
    pts_ny = [(0.0, y_face), (ndist * 3, y_face + (y_end - y_face) * 3),
              (ndist * 3, y_face + side * 20), (0.0, y_face + side * 20)]
    pl = cq.Plane(origin=(c1[0] - ux * 40, 0, c1[1] - uz * 40),
                  xDir=(nx, 0, nz), normal=(ux, 0, uz))
    sgn = 1 if pl.yDir.y > 0 else -1
    cutter = cq.Workplane(pl).polyline([(n, sgn * y) for (n, y) in pts_ny]).close().extrude(80)
    body = body.cut(cutter)

# soften the chisel: round the edges of the chamfer faces (except where they
# meet the plate faces, which stay crisp)
_cn = []
for side in (-1, 1):
    v = cq.Vector(nx * (W / 2 - TIP_Y), side * ndist, nz * (W / 2 - TIP_Y))
    _cn.append(v.normalized())
_tip_edges = []
for f in body.faces().vals():
    if f.geomType() != "PLANE":
        continue
    fn = f.normalAt()
    if any(abs(fn.dot(c)) > 0.999 for c in _cn):
        for e in f.Edges():
            m = e.Center()
            if abs(abs(m.y) - W / 2) > 0.5:
                _tip_edges.append(e)
if _tip_edges:
    try:
        body = body.newObject(_tip_edges).fillet(TIP_FILLET)
    except Exception:
        pass

# ---------------- bolt holes ----------------
for h in (H_top, H_mid, H_bot):
    body = body.cut(cq.Workplane("XZ").center(h[0], h[1]).circle(BIG_D / 2).extrude(W, both=True))
    body = body.cut(xz_wp(-W / 2 - 1).center(*Lp(h)).circle(CB_D / 2).extrude(CB_DEPTH + 1))
    body = body.cut(cq.Workplane().add(cq.Solid.makeCone(
        CB_D / 2 + CB_CH + 0.5, CB_D / 2, CB_CH + 0.5,
        cq.Vector(h[0], -W / 2 - 0.5, h[1]), cq.Vector(0, 1, 0))))
    hex_pts = [(h[0] + HEX_R * math.cos(math.radians(HEX_ROT + 60 * i)),
                h[1] + HEX_R * math.sin(math.radians(HEX_ROT + 60 * i))) for i in range(6)]
    body = body.cut(xz_wp(W / 2 - HEX_DEPTH).polyline([Lp(q) for q in hex_pts]).close()
                    .extrude(HEX_DEPTH + 1))

for h in small_holes:
    body = body.cut(cq.Workplane("XZ").center(h[0], h[1]).circle(SMALL_D / 2).extrude(W, both=True))

result = body
